import math
import cadquery as cq

# ======================= driving dimensions (mm) =======================
# Arm: faceted bar along X, drooping toward +X.  It is lofted between two hexagonal end
# sections given as (y, z) pairs in the order
#   top(-Y), top(+Y), shoulder(+Y), bottom(+Y), bottom(-Y), shoulder(-Y)
ARM_X0 = 0.0
ARM_X1_TOP, ARM_X1_BOT = 208.8, 213.0     # +X end face leans outward toward the bottom
SEC0 = [(-47.0, 150.4), (45.0, 150.4), (46.0, 126.5), (46.0, 110.5), (-49.5, 110.5), (-48.5, 126.5)]
SEC1 = [(-46.5, 129.5), (46.5, 129.5), (48.0, 125.5), (51.0, 96.5), (-51.0, 96.5), (-48.0, 125.5)]
# big bevel along the arm's upper -Y edge: plane through two points at its -X start and one
# point at the +X end where it runs out
BEVEL_P1, BEVEL_P2, BEVEL_P3 = (21.5, -33.0, 148.4), (23.2, -48.5, 125.8), (208.0, -47.0, 127.5)
BEVEL_X0 = 21.5
# blunt -X nose: two vertical corner chamfers (each a line through two plan points) and an
# end face that leans back toward the top (x at the arm bottom / top)
NOSE_PLUS = ((16.0, 47.5), (3.5, 16.0))
NOSE_MINUS = ((3.5, -21.0), (27.0, -53.0))
NOSE_X_BOT, NOSE_X_TOP = 0.5, 5.0

# Trough: open toward +X, horizontal floor
FLOOR_Z = 112.0
FLOOR_X0 = 113.0                     # foot of the -X end wall
FLOOR_HW0, FLOOR_HW1 = 17.0, 27.0    # floor half width at FLOOR_X0 and at x=206
SLOPE_END = 0.68                     # -X end wall run per unit rise
# side wall run per unit rise at the -X and +X ends of the trough (walls are slightly twisted)
SLOPE_PLUS = (0.80, 1.05)
SLOPE_MINUS = (0.62, 1.05)
POCKET_H = 34.0                      # pocket tool stops below the boss top
SLOT_X0, SLOT_X1, SLOT_HW = 113.0, 123.5, 16.0          # slot through the floor
LIP_X, LIP_DROP = 207.0, 8.0         # bevel where the floor runs out at +X

# Boss on the -X end: rounded square with a broad bevelled top
BOSS_X0, BOSS_X1, BOSS_Y0, BOSS_Y1 = 18.0, 93.0, -35.0, 42.0
BOSS_TOP = (27.0, 75.0, -22.0, 25.0)  # flat top x0, x1, y0, y1
BOSS_Z_BEVEL, BOSS_Z_TOP = 148.0, 160.6
BOSS_R_BASE, BOSS_R_TOP = 14.0, 4.0

# Lower block under the +X half of the arm (pentagonal section with slanted underside)
BLOCK_X0, BLOCK_X1 = 124.0, 208.0
BLOCK_SEC = [(40.0, 110.0), (48.0, 28.0), (27.0, 7.3), (-48.0, 23.5), (-40.0, 110.0)]

# Knurled ring (modelled plain): a conical wheel, trimmed flat where it meets the trough end,
# then a thin collar and the polygonal head; common axis along X
AXIS_Z = 57.6
RING_X0, RING_X1, RING_R0, RING_R1, RING_TOP = 207.5, 218.5, 58.0, 50.0, 108.0
COLLAR_X1, COLLAR_R = 221.0, 48.6
HEAD_X0, HEAD_X1 = 221.0, 233.9
# head outline (y, z): a slightly irregular seven-sided knob, as measured from the end view
HEAD_PTS = [(-22.6, 101.4), (13.8, 104.5), (47.0, 68.5), (45.0, 33.5), (2.7, 10.2), (-31.7, 21.5), (-46.0, 73.1)]

VIEW = {"azimuth": 45, "elevation": 26}


def wire(pts):
    return cq.Wire.makePolygon([cq.Vector(*p) for p in pts], close=True)


def rounded_rect_wire(x0, x1, y0, y1, r, z):
    w = cq.Workplane("XY", origin=(0, 0, z)).center((x0 + x1) / 2, (y0 + y1) / 2).rect(x1 - x0, y1 - y0).val()
    return w.fillet2D(r, w.Vertices())


def x_end(z):
    """x of the leaning +X end face at height z"""
    zt, zb = SEC1[0][1], SEC1[3][1]
    return ARM_X1_TOP + (ARM_X1_BOT - ARM_X1_TOP) * (zt - z) / (zt - zb)


# ---------------- arm ----------------
w0 = wire([(ARM_X0 - 5.0, y, z) for y, z in SEC0])
w1 = wire([(x_end(z), y, z) for y, z in SEC1])
arm = cq.Workplane("XY").add(cq.Solid.makeLoft([w0, w1], True))

# blunt nose: cut away everything on the -X side of the two corner chamfers and the leaning end face
def _extend(p, q, y):
    """point on line p->q (continued past q) at ordinate y"""
    return (q[0] + (q[0] - p[0]) * (y - q[1]) / (q[1] - p[1]), y)


def _at_x(p, q, x):
    # point on line p-q at abscissa x
    return (x, p[1] + (q[1] - p[1]) * (x - p[0]) / (q[0] - p[0]))


def nose_wire(z):
    xe = NOSE_X_BOT + (NOSE_X_TOP - NOSE_X_BOT) * (z - SEC0[4][1]) / (SEC0[0][1] - SEC0[4][1])
    pts = [(-20.0, 90.0), _extend(NOSE_PLUS[1], NOSE_PLUS[0], 90.0), _at_x(*NOSE_PLUS, xe),
           _at_x(*NOSE_MINUS, xe), _extend(NOSE_MINUS[0], NOSE_MINUS[1], -90.0), (-20.0, -90.0)]
    return wire([(x, y, z) for x, y in pts])


nose_cut = cq.Workplane("XY").add(cq.Solid.makeLoft([nose_wire(95.0), nose_wire(165.0)], True))
arm = arm.cut(nose_cut)

# bevel on the upper -Y edge (starts just behind the nose)
p1, p2, p3 = (cq.Vector(*p) for p in (BEVEL_P1, BEVEL_P2, BEVEL_P3))
bn = (p2 - p1).cross(p3 - p1).normalized()
if bn.y > 0:
    bn = -bn
bevel_plane = cq.Plane(origin=p1, xDir=(p3 - p1).normalized(), normal=bn)
bevel_cut = cq.Workplane(bevel_plane).rect(600, 600).extrude(80)
bevel_cut = bevel_cut.intersect(
    cq.Workplane("XY").box(400, 200, 200, centered=False).translate((BEVEL_X0, -200, 50))
)
arm = arm.cut(bevel_cut)

# ---------------- boss ----------------
boss_low = (
    cq.Workplane("XY", origin=(0, 0, 125.0))
    .center((BOSS_X0 + BOSS_X1) / 2, (BOSS_Y0 + BOSS_Y1) / 2)
    .rect(BOSS_X1 - BOSS_X0, BOSS_Y1 - BOSS_Y0)
    .extrude(BOSS_Z_BEVEL - 125.0)
    .edges("|Z")
    .fillet(BOSS_R_BASE)
)
w_lo = rounded_rect_wire(BOSS_X0, BOSS_X1, BOSS_Y0, BOSS_Y1, BOSS_R_BASE, BOSS_Z_BEVEL)
tx0, tx1, ty0, ty1 = BOSS_TOP
w_hi = rounded_rect_wire(tx0, tx1, ty0, ty1, BOSS_R_TOP, BOSS_Z_TOP)
boss_top = cq.Workplane("XY").add(cq.Solid.makeLoft([w_lo, w_hi], True))
body = arm.union(boss_low).union(boss_top)

# ---------------- lower block ----------------
block = cq.Workplane("XY").add(
    cq.Solid.makeLoft(
        [wire([(BLOCK_X0, y, z) for y, z in BLOCK_SEC]), wire([(BLOCK_X1, y, z) for y, z in BLOCK_SEC])], True
    )
)
body = body.union(block)

# ---------------- trough pocket ----------------
XE = 245.0


def hw(x):
    return FLOOR_HW0 + (FLOOR_HW1 - FLOOR_HW0) * (x - FLOOR_X0) / (206.0 - FLOOR_X0)


H = POCKET_H
floor_w = wire([(FLOOR_X0, -hw(FLOOR_X0), FLOOR_Z), (XE, -hw(XE), FLOOR_Z),
                (XE, hw(XE), FLOOR_Z), (FLOOR_X0, hw(FLOOR_X0), FLOOR_Z)])
top_w = wire([
    (FLOOR_X0 - SLOPE_END * H, -hw(FLOOR_X0) - SLOPE_MINUS[0] * H, FLOOR_Z + H),
    (XE, -hw(XE) - SLOPE_MINUS[1] * H, FLOOR_Z + H),
    (XE, hw(XE) + SLOPE_PLUS[1] * H, FLOOR_Z + H),
    (FLOOR_X0 - SLOPE_END * H, hw(FLOOR_X0) + SLOPE_PLUS[0] * H, FLOOR_Z + H),
])
pocket = cq.Solid.makeLoft([floor_w, top_w], True)
body = body.cut(cq.Workplane("XY").add(pocket))

# slot through the floor at the foot of the end wall
slot = cq.Workplane("XY").box(SLOT_X1 - SLOT_X0, 2 * SLOT_HW, 40.0).translate(((SLOT_X0 + SLOT_X1) / 2, 0, FLOOR_Z))
body = body.cut(slot)

# bevel where the floor runs out at +X (only between the walls)
lip_hw = hw(ARM_X1_TOP)
lip = (
    cq.Workplane("XZ", origin=(0, lip_hw, 0))
    .polyline([(LIP_X, FLOOR_Z + 0.5), (XE, FLOOR_Z + 0.5), (XE, FLOOR_Z - LIP_DROP * (XE - LIP_X) / 12.0)])
    .close()
    .extrude(2 * lip_hw)
)
body = body.cut(lip)

# ---------------- knurled ring (plain cone, trimmed under the trough end) and collar ----------------
ring = (
    cq.Workplane("YZ", origin=(RING_X0, 0, AXIS_Z))
    .circle(RING_R0)
    .workplane(offset=RING_X1 - RING_X0)
    .circle(RING_R1)
    .loft()
    .cut(cq.Workplane("XY").box(40, 200, 100).translate(((RING_X0 + RING_X1) / 2, 0, RING_TOP + 50)))
)
collar = cq.Workplane("YZ", origin=(RING_X1 - 0.5, 0, AXIS_Z)).circle(COLLAR_R).extrude(COLLAR_X1 - RING_X1 + 1.0)
body = body.union(ring).union(collar)

# ---------------- polygonal head ----------------
head = cq.Workplane("XY").add(
    cq.Solid.makeLoft([wire([(HEAD_X0, y, z) for y, z in HEAD_PTS]), wire([(HEAD_X1, y, z) for y, z in HEAD_PTS])], True)
)
body = body.union(head)

result = body
